import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
DISK_D = 100.0          # base disk diameter
DISK_T = 17.0           # base disk thickness
COLLAR_D = 40.0         # raised collar diameter
COLLAR_H = 6.5          # collar height above disk
SQ_SIDE = 26.7          # square post side
SQ_H = 33.5             # square post height above collar
SQ_ROT = 37.5           # square post rotation about Z (deg)
HOLE_D = 18.0           # through bore diameter

# underside flower pocket
POCKET_DEPTH = 13.3
N_LOBES = 9
LOBE_TIP_R = 43.6       # radius to outermost point of a lobe
LOBE_R = 7.5            # lobe arc radius
VALLEY_IN_R = 35.5      # radius to innermost point of a valley
LOBE_PHASE = SQ_ROT     # angle of first lobe (deg), aligned with the square post

VIEW = {"azimuth": 45, "elevation": 26}


def flower_wire(n, tip_r, r1, valley_in_r, phase_deg=0.0):
    """Closed outline of n lobes (arc radius r1, outermost point at tip_r) joined
    by tangent valley arcs whose innermost point lies at valley_in_r."""
    R1 = tip_r - r1                 # lobe circle centre radius
    half = math.pi / n
    c = math.cos(half)
    v = valley_in_r
    # valley circle (radius r2, centre radius v + r2) externally tangent to lobe circle:
    # (r1 + r2)^2 = R1^2 + (v + r2)^2 - 2 R1 (v + r2) cos(half)
    r2 = (R1 * R1 + v * v - 2 * R1 * v * c - r1 * r1) / (2 * r1 - 2 * v + 2 * R1 * c)
    R2 = v + r2
    ph = math.radians(phase_deg)

    def pol(r, ang):
        return (r * math.cos(ang), r * math.sin(ang))

    def tp(P, Q):
        dx, dy = Q[0] - P[0], Q[1] - P[1]
        L = math.hypot(dx, dy)
        return (P[0] + r1 * dx / L, P[1] + r1 * dy / L)

    segs = []
    for k in range(n):
        a = 2 * math.pi * k / n + ph
        P = pol(R1, a)
        Q = pol(R2, a + half)
        Qp = pol(R2, a - half)
        P2 = pol(R1, a + 2 * half)
        segs.append((tp(P, Qp), pol(tip_r, a), tp(P, Q), pol(v, a + half), tp(P2, Q)))
    wp = cq.Workplane("XY").moveTo(*segs[0][0])
    for (t_in, tip, t_out, vin, t_next) in segs:
        wp = wp.threePointArc(tip, t_out).threePointArc(vin, t_next)
    return wp.close()


# base disk (cylinder seams turned to the back-left, purely cosmetic)
SEAM_ANG = 135.0
disk = (
    cq.Workplane("XY").circle(DISK_D / 2).extrude(DISK_T)
    .rotate((0, 0, 0), (0, 0, 1), SEAM_ANG)
)
# raised collar
collar = (
    cq.Workplane("XY").workplane(offset=DISK_T).circle(COLLAR_D / 2).extrude(COLLAR_H)
    .rotate((0, 0, 0), (0, 0, 1), SEAM_ANG)
)
body = disk.union(collar)
# square post
post = (
    cq.Workplane("XY")
    .workplane(offset=DISK_T + COLLAR_H)
    .transformed(rotate=(0, 0, SQ_ROT))
    .rect(SQ_SIDE, SQ_SIDE)
    .extrude(SQ_H)
)
body = body.union(post)

# underside flower pocket
pocket = flower_wire(N_LOBES, LOBE_TIP_R, LOBE_R, VALLEY_IN_R, LOBE_PHASE).extrude(POCKET_DEPTH)
body = body.cut(pocket)

# through bore
total_h = DISK_T + COLLAR_H + SQ_H
bore = cq.Workplane("XY").circle(HOLE_D / 2).extrude(total_h + 2).translate((0, 0, -1))
body = body.cut(bore)

result = body
